import math
import cadquery as cq

# =====================================================================
#  Drum actuator: cylindrical drum with front cap, back mounting plate
#  with a tilted tab, and a tilted gear-motor housing on the +X side.
#  Drum axis = Y (front cap at -Y).  Dimensions in mm.
# =====================================================================
R = 30.0                 # drum radius
R_DRUM = R - 0.25        # drum shell radius (slightly under the cap rim)
R_IN = 0.86 * R          # inner (core) radius -> drum wall thickness
CAP_T = 0.187 * R        # front cap thickness
RING_Y = 0.34 * R        # end of the closed front ring of the drum wall
Y_PLATE = 1.57 * R       # front face of back plate
PLATE_T = 0.15 * R       # back plate thickness
TILT = 18.0              # tilt of tab / housing axis in the XZ plane (deg)

# mounting tab (part of the back plate)
TAB_P0, TAB_P1 = 0.126 * R, 0.98 * R     # tab band (perpendicular offsets)
TAB_END = 2.02 * R                       # tab length from drum axis
TAB_R = 0.15 * R                         # tab corner radius
HOLE_A, HOLE_D = 1.69 * R, 0.17 * R      # mounting hole

# big side window on the -X side of the drum wall, exposing the core
SIDE_WIN = (110.0, 197.0)                # angular extent of the wall opening
SIDE_Y0 = RING_Y - 0.01 * R              # side window starts just behind the front ring
FLAT_HOLE_D = 0.09 * R                   # fixing holes in the exposed core
HEX_S = 0.15 * R                         # hex recess across flats

# shallow tapered flat on the upper +X side of the drum
FACET_ANG = 65.5                         # facet normal direction in XZ (deg)
FACET_H0 = 0.953 * R                     # facet distance from axis at the front
FACET_H1 = 0.987 * R                     # ... and at the back plate
FACET_Y1 = 1.45 * R                      # facet stops short of the back plate

# windows in the drum wall just above the housing (angles in deg)
WIN1 = (10.0, 18.5, RING_Y + 0.01 * R, 0.80 * R)
WIN2 = (5.0, 18.5, 1.20 * R, Y_PLATE)
# slot in the drum wall just below the housing
LOWSLOT = (-72.0, -53.0, RING_Y, Y_PLATE)

# gear motor housing ------------------------------------------------
HS_P0, HS_P1 = -0.95 * R, -0.133 * R     # housing band (perpendicular)
HS_END = 2.06 * R                        # motor block length from drum axis (front part)
HS_END2 = 2.15 * R                       # back part of the motor block sticks out a little
HS_YS = 0.94 * R                         # start of the back part (chamfered step)
STEP_CH = 0.06 * R                       # chamfer of that step
HS_Y0 = CAP_T                            # housing front face
HS_YM = 1.20 * R                         # back of motor block
HS_YG = 1.20 * R                         # start of gear head flange
HS_YF = 1.29 * R                         # end of gear flange
HS_YB = 1.53 * R                         # end of gear box
GB_END = 1.92 * R                        # gear box length
GB_P = (-0.84 * R, -0.22 * R)            # gear box band
FL_END = 2.15 * R                        # servo mounting tab length
FL_P = (-0.90 * R, -0.22 * R)            # mounting tab band
FL_FIL = 0.08 * R                        # mounting tab corner rounding
FL_SLOT = (-0.61 * R, -0.49 * R, 0.10 * R)  # open slot in the tab end
FIL_TOP, FIL_BOT = 0.12 * R, 0.12 * R
TOPREC_A = (0.60 * R, 1.55 * R)          # shallow recess in the housing top
TOPREC_Y = (RING_Y + 0.01 * R, 1.20 * R)
TOPREC_D = 0.07 * R
SLOT_P0, SLOT_P1 = -0.66 * R, -0.42 * R  # connector slot in the end face
SLOT_D = 0.15 * R
SLOT_Y0 = RING_Y
PLUG_Y = (0.40 * R, 0.60 * R)            # 3-pin plug position in the slot
BOTPOCKET_A = (0.97 * R, 1.50 * R)       # pocket in the housing underside
BOTPOCKET2_A = (0.25 * R, 0.80 * R)      # second pocket at the drum junction
BOTPOCKET_Y = (RING_Y, 1.20 * R)
BOTPOCKET_D = 0.10 * R

SHAFT_X, SHAFT_Z = 1.78 * R, -0.04 * R   # output shaft axis
SHAFT_D = 0.20 * R
SHAFT_TOP = 1.735 * R
BOSS_D = 0.50 * R                        # round boss around the shaft
BOSS_TOP = 1.60 * R

ca, sa = math.cos(math.radians(TILT)), math.sin(math.radians(TILT))


def ap(a, p):
    """(along, perpendicular) in the tilted frame -> (X, Z)."""
    return (a * ca - p * sa, a * sa + p * ca)


def box_ap(a0, a1, p0, p1, y0, y1, fil=None, cham=None):
    """Box aligned with the tilted frame (a along X, p along Z before tilt).
    fil: list of (selector, radius) applied before the tilt;
    cham: optional (selector, length1, length2) chamfer applied after the fillets."""
    ac, pc = (a0 + a1) / 2, (p0 + p1) / 2
    x, z = ap(ac, pc)
    b = cq.Workplane("XY").box(a1 - a0, y1 - y0, p1 - p0)
    for sel, r in (fil or []):
        b = b.edges(sel).fillet(r)
    if cham:
        b = b.edges(cham[0]).chamfer(cham[1], cham[2])
    b = b.rotate((0, 0, 0), (0, 1, 0), -TILT)
    return b.translate((x, (y0 + y1) / 2, z))


def box_rot(ang, r0, r1, t0, t1, y0, y1):
    """Box in a frame rotated by ang (deg) about Y: r radial, t tangential."""
    b = (cq.Workplane("XY").box(r1 - r0, y1 - y0, t1 - t0)
         .translate(((r0 + r1) / 2, (y0 + y1) / 2, (t0 + t1) / 2)))
    return b.rotate((0, 0, 0), (0, 1, 0), -ang)


def disc(r, y0, y1, x=0.0, z=0.0):
    return (cq.Workplane("XZ").center(x, z).circle(r).extrude(y1 - y0)
            .translate((0, y1, 0)))


def sector(r0, r1, f0, f1, y0, y1):
    """Annular sector (angles in deg, measured from +X towards +Z)."""
    def pt(r, f):
        return (r * math.cos(math.radians(f)), r * math.sin(math.radians(f)))
    fm = (f0 + f1) / 2
    w = (cq.Workplane("XZ").moveTo(*pt(r0, f0)).lineTo(*pt(r1, f0))
         .threePointArc(pt(r1, fm), pt(r1, f1)).lineTo(*pt(r0, f1))
         .threePointArc(pt(r0, fm), pt(r0, f0)).close().extrude(y1 - y0))
    return w.translate((0, y1, 0))


# ---------------- front cap + drum + back plate ----------------
# (main discs turned 180 deg so their seam lies on the -X side)
cap = disc(R, 0.0, CAP_T).rotate((0, 0, 0), (0, 1, 0), 180)
drum = disc(R_DRUM, CAP_T, Y_PLATE).rotate((0, 0, 0), (0, 1, 0), 180)
# tapered facet: plane cos(f)X + sin(f)Z - k*Y = FACET_H0 - k*CAP_T
_k = (FACET_H1 - FACET_H0) / (Y_PLATE - CAP_T)
_f = math.radians(FACET_ANG)
_N = cq.Vector(math.cos(_f), -_k, math.sin(_f))
_d = FACET_H0 - _k * CAP_T
_p0 = _N * (_d / _N.Length ** 2)
_pl = cq.Plane(origin=_p0.toTuple(), xDir=(-math.sin(_f), 0, math.cos(_f)),
               normal=_N.normalized().toTuple())
facet_cut = cq.Workplane(_pl).rect(6 * R, 6 * R).extrude(R)
facet_cut = facet_cut.intersect(cq.Workplane("XY").box(4 * R, FACET_Y1, 4 * R)
                                .translate((0, FACET_Y1 / 2, 0)))
drum = drum.cut(facet_cut)

tab = box_ap(-TAB_END, 0, TAB_P0, TAB_P1, Y_PLATE, Y_PLATE + PLATE_T,
             [("|Y and <X", TAB_R)])
plate = disc(R, Y_PLATE, Y_PLATE + PLATE_T).rotate((0, 0, 0), (0, 1, 0), 180).union(tab)
hx, hz = ap(-HOLE_A, (TAB_P0 + TAB_P1) / 2)
plate = plate.cut(disc(HOLE_D / 2, Y_PLATE - 1, Y_PLATE + PLATE_T + 1, hx, hz))

# ---------------- gear motor housing ----------------
end_fil = [("|Y and >X and >Z", FIL_TOP), ("|Y and >X and <Z", FIL_BOT)]
motor = box_ap(0, HS_END, HS_P0, HS_P1, HS_Y0, HS_YS + 0.5 * STEP_CH, end_fil)
motor = motor.union(box_ap(0, HS_END2, HS_P0, HS_P1, HS_YS, HS_YM, end_fil,
                           ("|Z and >X and <Y", 1.4 * STEP_CH, STEP_CH)))
gflange = box_ap(0, FL_END, FL_P[0], FL_P[1], HS_YG, HS_YF, [("|Y and >X", FL_FIL)])
gflange = gflange.cut(box_ap(FL_END - FL_SLOT[2], FL_END + 1, FL_SLOT[0], FL_SLOT[1],
                             HS_YG - 1, HS_YF + 1))
gbox = box_ap(0, GB_END, GB_P[0], GB_P[1], HS_YF, HS_YB)
housing = motor.union(gflange).union(gbox)

sx, sz = SHAFT_X, SHAFT_Z
boss = disc(BOSS_D / 2, HS_YB - 0.02 * R, BOSS_TOP, sx, sz)
shaft = disc(SHAFT_D / 2, BOSS_TOP - 0.01 * R, SHAFT_TOP, sx, sz)

part = cap.union(drum).union(plate).union(housing).union(boss).union(shaft)

# ---------------- cuts ----------------
# big -X window through the drum wall (the core stays, showing its surface)
part = part.cut(sector(R_IN - 0.01, R + 1, SIDE_WIN[0], SIDE_WIN[1], SIDE_Y0, Y_PLATE))
# fixing holes and a hex nut recess in the exposed core surface
for (yy, ff) in [(0.45, 113.0), (0.45, 152.0), (0.48, 188.0)]:
    hole = (cq.Workplane("YZ").circle(FLAT_HOLE_D / 2).extrude(0.3 * R)
            .translate((R_IN - 0.2 * R, yy * R, 0))
            .rotate((0, 0, 0), (0, 1, 0), -ff))
    part = part.cut(hole)
hexr = (cq.Workplane("YZ").polygon(6, HEX_S / math.cos(math.radians(30)))
        .extrude(0.25 * R).translate((R_IN - 0.1 * R, 0.98 * R, 0))
        .rotate((0, 0, 0), (0, 1, 0), -146.0))
part = part.cut(hexr)

# windows through the drum wall above and below the housing
for (f0, f1, y0, y1) in (WIN1, WIN2, LOWSLOT):
    part = part.cut(sector(R_IN, R + 0.2 * R, f0, f1, y0, y1))

# connector slot along Y in the end face, with a 3-pin plug at its front
part = part.cut(box_ap(HS_END - SLOT_D, HS_END2 + 1, SLOT_P0, SLOT_P1, SLOT_Y0, HS_YM + 1))
part = part.union(box_ap(HS_END - SLOT_D, HS_END - 0.05 * R, SLOT_P0 + 0.015 * R,
                         SLOT_P1 - 0.015 * R, PLUG_Y[0], PLUG_Y[1]))
for k in range(3):
    pp = SLOT_P0 + (k + 0.5) * (SLOT_P1 - SLOT_P0) / 3
    px, pz = ap(HS_END - 0.05 * R, pp)
    pin = (cq.Workplane("YZ").circle(0.032 * R).extrude(0.05 * R)
           .rotate((0, 0, 0), (0, 1, 0), -TILT)
           .translate((px, (PLUG_Y[0] + PLUG_Y[1]) / 2, pz)))
    part = part.union(pin)

# shallow recess in the top of the motor block
part = part.cut(box_ap(TOPREC_A[0], TOPREC_A[1], HS_P1 - TOPREC_D, HS_P1 + 1,
                       TOPREC_Y[0], TOPREC_Y[1]))

# pocket in the underside of the housing
part = part.cut(box_ap(BOTPOCKET_A[0], BOTPOCKET_A[1], HS_P0 - 1, HS_P0 + BOTPOCKET_D,
                       BOTPOCKET_Y[0], BOTPOCKET_Y[1]))
part = part.cut(box_ap(BOTPOCKET2_A[0], BOTPOCKET2_A[1], HS_P0 - 0.3 * R, HS_P0 + BOTPOCKET_D,
                       BOTPOCKET_Y[0], 1.15 * R))

result = part

VIEW = {"azimuth": 45, "elevation": 26}
